import math
import cadquery as cq

# =====================================================================
#  Asymmetric conical fairing / nose cover
#  - thin lofted skin, open at a tilted elliptic top face
#  - floor plate with a large rectangular opening
#  - three internal screw bosses (right, back, left) with counterbored
#    holes drilled straight down through the skin
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
BASE_HALF_W = 49.8      # half width of base (X)
BASE_FRONT = 25.0       # base extent toward front (-Y) from design centre
BASE_BACK = 50.8        # base extent toward back (+Y) from design centre
APEX_Z = 89.1           # virtual apex height (front view flanks)
SIDE_EXP = 0.906        # front-view flank curvature exponent

BACK_Y0 = -10.5         # back profile: elliptic arc centre (Y)
BACK_C = 89.4           # back profile: elliptic arc half height
FRONT_K = 0.0074        # front profile: Bf = BASE_FRONT - K*z^P
FRONT_P = 1.744

YJ_TOP = 5.2            # widest point of a section drifts back with height
YJ_EXP = 2.0            #   Yj = YJ_TOP * (z / TOP_CZ)^YJ_EXP

# section shape exponents  y = B*(1-|x/A|^n)^(1/m)
BACK_N0, BACK_M0 = 2.64, 1.46   # back half at the base
FRONT_N0, FRONT_M0 = 2.0, 2.0   # front half at the base
TOP_N, TOP_M = 2.0, 2.0         # both halves high up (ellipse)
BLEND_Z = 70.0                  # height over which the shape blends

# tilted top face (elliptic ring)
TOP_TILT = 24.6         # deg, plane rises toward the back
TOP_CY = -1.2           # centre of top ellipse (Y)
TOP_CZ = 80.8           # centre of top ellipse (Z)
TOP_AX = 5.3            # outer semi-axis across (X)
TOP_AS = 10.5           # outer semi-axis along the slope

WALL = 1.8              # skin / floor thickness
RING_X = 1.85           # ring width of top face across
RING_S = 2.0            # ring width of top face along slope
MOUTH_LIFT = 0.1        # inner loft overshoot above the top face

RECT_W = 64.0           # rectangular opening in floor (X)
RECT_D = 45.0           # (Y)
RECT_YC = 8.3           # centre of opening (Y)

HOLE_R = 41.0           # bolt circle radius (holes at right, back, left)
BOSS_D = 9.0            # internal screw boss diameter
ACCESS_D = 6.0          # counterbore / access bore
CBORE_Z = 4.0           # height of the counterbore floor
SCREW_D = 3.0           # screw clearance hole

# loft stations: (pivot Z on the design centre line, tilt in degrees)
STATIONS = [(0.0, 0.0), (22.0, 0.0), (44.0, 0.0), (64.0, 12.0), (74.0, 20.0)]
N_HALF = 10             # spline points per half station


# ---------------- analytic description of the skin ----------------
def half_w(z):
    return BASE_HALF_W * max(1e-6, 1.0 - z / APEX_Z) ** SIDE_EXP


def back_ext(z):
    a = BASE_BACK - BACK_Y0
    return BACK_Y0 + a * math.sqrt(max(0.0, 1.0 - (z / BACK_C) ** 2))


def front_ext(z):
    return BASE_FRONT - FRONT_K * max(z, 0.0) ** FRONT_P


def junction(z):
    return YJ_TOP * (max(z, 0.0) / TOP_CZ) ** YJ_EXP


def shape_exp(z):
    w = min(1.0, max(0.0, z / BLEND_Z))
    nb = BACK_N0 + (TOP_N - BACK_N0) * w
    mb = BACK_M0 + (TOP_M - BACK_M0) * w
    nf = FRONT_N0 + (TOP_N - FRONT_N0) * w
    mf = FRONT_M0 + (TOP_M - FRONT_M0) * w
    return nb, mb, nf, mf


def _slope(f, z, h=1e-3):
    z0 = max(0.0, z - h)
    return (f(z + h) - f(z0)) / (z + h - z0)


def skin_pt(phi, z, t=0.0):
    """Point of the skin at height z and angle phi (0 = +X, 90 deg = back).
    t > 0 gives the inner skin: each principal extent is pulled in by the
    horizontal distance that yields a wall of normal thickness t."""
    A = half_w(z) - t * math.sqrt(1 + _slope(half_w, z) ** 2)
    bb = back_ext(z) - t * math.sqrt(1 + _slope(back_ext, z) ** 2)
    bf = front_ext(z) - t * math.sqrt(1 + _slope(front_ext, z) ** 2)
    A = max(A, 0.05)
    yj = junction(z)
    bb = max(bb, yj + 0.05)
    bf = max(bf, -yj + 0.05)
    nb, mb, nf, mf = shape_exp(z)
    c = math.cos(phi)
    if math.sin(phi) >= 0:
        y = yj + (bb - yj) * max(0.0, 1 - abs(c) ** nb) ** (1.0 / mb)
    else:
        y = yj - (bf + yj) * max(0.0, 1 - abs(c) ** nf) ** (1.0 / mf)
    return (A * c, y, z)


# angular stations around a section; the outer skin starts on the back centre
# line, the inner skin on the front centre line, so the loft seams stay out
# of sight
def angles(start):
    return [start + 2 * math.pi * i / (2 * N_HALF) for i in range(2 * N_HALF)]


PHIS_OUT = angles(math.pi / 2)
PHIS_IN = angles(-math.pi / 2)


def wire_from(pts):
    # one common (uniform) parameterisation for every station keeps the loft
    # rulings running along constant angle
    edge = cq.Edge.makeSpline(
        [cq.Vector(*p) for p in pts], periodic=True, parameters=list(range(len(pts) + 1))
    )
    return cq.Wire.assembleEdges([edge])


def station(pz, tilt, t=0.0):
    """Closed section of the skin cut by a plane through (Y=TOP_CY, Z=pz)
    tilted by `tilt` degrees about X (rising toward the back)."""
    k = math.tan(math.radians(tilt))
    phis = PHIS_IN if t > 0 else PHIS_OUT
    pts = []
    for phi in phis:
        lo, hi = 0.0, APEX_Z - 0.5
        for _ in range(60):
            mid = 0.5 * (lo + hi)
            p = skin_pt(phi, mid, t)
            if p[2] - (pz + k * (p[1] - TOP_CY)) > 0:
                hi = mid
            else:
                lo = mid
        pts.append(skin_pt(phi, 0.5 * (lo + hi), t))
    return wire_from(pts)


def top_ellipse(ax, as_, lift=0.0, phis=PHIS_OUT):
    """Ellipse lying in the tilted top plane (optionally lifted along its
    normal)."""
    a = math.radians(TOP_TILT)
    sy, sz = math.cos(a), math.sin(a)          # in-plane slope direction
    ny, nz = -math.sin(a), math.cos(a)         # plane normal
    cy = TOP_CY + lift * ny
    cz = TOP_CZ + lift * nz
    pts = []
    for phi in phis:
        u = ax * math.cos(phi)
        v = as_ * math.sin(phi)
        pts.append((u, cy + v * sy, cz + v * sz))
    return wire_from(pts)


# ---------------- outer body (skin loft, capped by the top face) ----------
outer_wires = [station(z, a) for z, a in STATIONS]
outer_wires.append(top_ellipse(TOP_AX, TOP_AS))
outer = cq.Workplane("XY").add(cq.Solid.makeLoft(outer_wires, False))

# ---------------- inner cavity ----------------
# same stations as the outer skin so that both lofts interpolate alike; the
# last station sits a hair above the top face so the cavity breaks out
inner_wires = [station(WALL * 0.5, 0.0, WALL)]
inner_wires += [station(z, a, WALL) for z, a in STATIONS[1:]]
inner_wires.append(
    top_ellipse(TOP_AX - RING_X, TOP_AS - RING_S, lift=MOUTH_LIFT, phis=PHIS_IN)
)
cavity = cq.Workplane("XY").add(cq.Solid.makeLoft(inner_wires, False))
cavity = cavity.intersect(
    cq.Workplane("XY")
    .box(300, 300, 200, centered=(True, True, False))
    .translate((0, 0, WALL))
)
body = outer.cut(cavity)

# ---------------- screw bosses (inside the skin) ----------------
hole_pts = [(HOLE_R, 0.0), (0.0, HOLE_R), (-HOLE_R, 0.0)]
bosses = (
    cq.Workplane("XY")
    .pushPoints(hole_pts)
    .circle(BOSS_D / 2)
    .extrude(APEX_Z)
    .intersect(outer)
)
body = body.union(bosses)

# ---------------- rectangular opening through the floor ----------------
opening = (
    cq.Workplane("XY")
    .center(0, RECT_YC)
    .rect(RECT_W, RECT_D)
    .extrude(WALL * 3)
    .translate((0, 0, -WALL))
)
body = body.cut(opening)

# ---------------- counterbored screw holes ----------------
access = (
    cq.Workplane("XY")
    .workplane(offset=CBORE_Z)
    .pushPoints(hole_pts)
    .circle(ACCESS_D / 2)
    .extrude(APEX_Z)
)
screw = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .pushPoints(hole_pts)
    .circle(SCREW_D / 2)
    .extrude(CBORE_Z + 2)
)
body = body.cut(access).cut(screw)

# ---------------- surface refinement for export ----------------
# The skin loft is a single span across its stations; inserting extra knots
# (an exact, shape-preserving refinement) gives downstream meshers more
# parameter lines to work with and smoother shading.
from cadquery.occ_impl.shapes import BRep_Tool, BRepTools

REFINE_SPANS = 12
solid = body.val()
BRepTools.Clean_s(solid.wrapped)
for face in solid.Faces():
    if face.geomType() != "BSPLINE":
        continue
    srf = BRep_Tool.Surface_s(face.wrapped)
    v0, v1 = srf.VKnot(1), srf.VKnot(srf.NbVKnots())
    for i in range(1, REFINE_SPANS):
        srf.InsertVKnot(v0 + (v1 - v0) * i / REFINE_SPANS, 1, 1e-9, True)

result = cq.Workplane("XY").add(solid)
